import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 50.0          # width (X)
H = 87.7          # height (Z)
D = 23.7          # flange depth from back face to front edge (Y)
T_F = 3.2         # flange thickness
T_BACK = 5.6      # back wall thickness at the rim
T_PLATE = 3.3     # back wall thickness inside the pocket
R1 = 5.5          # inner bend radius at rim level
RIM_H = T_BACK - T_PLATE
R2 = R1 + RIM_H   # inner bend radius at pocket level
RIM_W = 3.5       # side rim width
NOTCH_KEEP = 1.7  # side rim width left at the notches
BOT_W = 2.3       # bottom rim width
R_BACK = 3.0      # rounding of the vertical back edges

NOTCH_LEN = 10.0
NOTCH_Z = [H - 24.6, H - 64.5]   # notch centres

SLOT_L, SLOT_W, SLOT_R = 13.4, 8.6, 3.0
SLOT_Y = -13.6                   # slot centre (back face at y = 0)

TAB_W, TAB_H, TAB_P = 8.7, 1.6, 2.0
TAB_X = 13.0

BOSS_R = 6.2
BOSS_L = 13.0
BOSS_DOME = 5.5                  # rounding of the free end (dome)
BOSS_Y = -6.7
BOSS_GAP = 1.0                   # gap between boss flat end and rim
TOP_BOSS_Z = H - 10.4
LOW_BOSS_Z = 16.4
PIN_D = 2.9
PIN_OFF = -2.5                   # pin hole offset from boss axis (Y)
PIN_DEPTH = BOSS_L - 0.7         # just breaks through the dome

# back face decoration: raised panels split by a cross shaped channel
CH_DEPTH = 0.6
CH_V_X = (-1.9, 2.3)             # vertical channel x-range
CH_H_Z = (59.8, 64.3)            # horizontal channel z-range
PANEL_TOP = 82.4                 # channel top / apex of the V facet
V_REACH = 23.0                   # V facet reaches the top edge at this |x|
CH_R = 4.0                       # rounding of the panel corners
CH_TAPER = 45.0                  # sloped channel walls
TXT = "OSRTT"
TXT_SIZE = 13.55
TXT_DEPTH = 0.5
TXT_X, TXT_Z = -12.5, 31.45

LATCH_HALF = 7.15                # bottom rim latch half width
SLIT = 0.5                       # groove width either side of the latch
SLIT_D = 0.6                     # groove depth into the rim front face
LATCH_P = 0.2                    # latch stands slightly proud

# ---------------- main L body (rim level) ----------------
body = (
    cq.Workplane("YZ")
    .moveTo(0, 0)
    .lineTo(0, H)
    .lineTo(-D, H)
    .lineTo(-D, H - T_F)
    .lineTo(-T_BACK - R1, H - T_F)
    .radiusArc((-T_BACK, H - T_F - R1), R1)
    .lineTo(-T_BACK, 0)
    .close()
    .extrude(W / 2, both=True)
)

# round the vertical back edges
body = body.edges("|Z").edges(
    cq.selectors.BoxSelector((-W, -0.1, -1), (W, 0.1, H + 1))
).fillet(R_BACK)

# ---------------- pocket (recess inside the rim) ----------------
y_far = -D - 5
pocket = (
    cq.Workplane("YZ")
    .moveTo(-T_PLATE, BOT_W)
    .lineTo(-T_PLATE, H - T_F - R2)
    .radiusArc((-T_PLATE - R2, H - T_F), -R2)
    .lineTo(y_far, H - T_F)
    .lineTo(y_far, BOT_W)
    .close()
    .extrude(W / 2 - RIM_W, both=True)
)
body = body.cut(pocket)

# ---------------- notches in the side rims ----------------
xin = W / 2 - RIM_W          # rim inner face
xout = W / 2 - NOTCH_KEEP    # notch bottom
for zc in NOTCH_Z:
    for sx in (-1, 1):
        n = (
            cq.Workplane("XY")
            .box(xout - xin + 0.01, T_BACK, NOTCH_LEN)
            .translate((sx * (xin + xout) / 2, -T_PLATE - T_BACK / 2, zc))
        )
        body = body.cut(n)

# ---------------- bottom rim latch (grooves + small lip) ----------------
for sx in (-1, 1):
    s = (
        cq.Workplane("XY")
        .box(SLIT, SLIT_D + 1.0, BOT_W + 2)
        .translate((sx * (LATCH_HALF + SLIT / 2), -T_BACK + SLIT_D - (SLIT_D + 1.0) / 2, BOT_W / 2))
    )
    body = body.cut(s)
lip = (
    cq.Workplane("XY")
    .box(2 * LATCH_HALF, LATCH_P, BOT_W)
    .translate((0, -T_BACK - LATCH_P / 2, BOT_W / 2))
)
body = body.union(lip)

# ---------------- tabs under the flange front edge ----------------
for sx in (-1, 1):
    tab = (
        cq.Workplane("XY")
        .box(TAB_W, TAB_P + 1.0, TAB_H)
        .translate((sx * TAB_X, -D - TAB_P / 2 + 0.5, H - T_F + TAB_H / 2))
    )
    body = body.union(tab)

# ---------------- slot through the flange ----------------
slot = (
    cq.Workplane("XY")
    .sketch()
    .rect(SLOT_L, SLOT_W)
    .vertices()
    .fillet(SLOT_R)
    .finalize()
    .extrude(T_F + 2)
    .translate((0, SLOT_Y, H - T_F - 1))
)
body = body.cut(slot)


# ---------------- bosses (dome ended cylinders along X) ----------------
def boss(x_flat, direction, zc):
    """Cylinder along X with a rounded (domed) free end, flat end at x_flat,
    extending in +X (direction=1) or -X (direction=-1)."""
    b = (
        cq.Workplane("YZ", origin=(x_flat, 0, 0))
        .center(BOSS_Y, zc)
        .circle(BOSS_R)
        .extrude(BOSS_L * direction)
    )
    b = b.faces(">X" if direction > 0 else "<X").edges().fillet(BOSS_DOME)
    hole = (
        cq.Workplane("YZ", origin=(x_flat - direction * 0.01, 0, 0))
        .center(BOSS_Y + PIN_OFF, zc)
        .circle(PIN_D / 2)
        .extrude(PIN_DEPTH * direction)
    )
    return b, hole


xr = W / 2 - RIM_W - BOSS_GAP
b1, h1 = boss(xr, -1, TOP_BOSS_Z)
b2, h2 = boss(-xr, 1, LOW_BOSS_Z)
body = body.union(b1).union(b2).cut(h1).cut(h2)


# ---------------- back face decoration ----------------
big = 3 * max(W, H)
vx0, vx1 = CH_V_X
hz0, hz1 = CH_H_Z
v_top = PANEL_TOP + CH_DEPTH          # channel floor ends at PANEL_TOP
ch = (
    cq.Sketch()
    .push([((vx0 + vx1) / 2, (v_top - big) / 2)])
    .rect(vx1 - vx0, v_top + big)
    .push([(0, (hz0 + hz1) / 2)])
    .rect(big, hz1 - hz0)
    .reset()
    .clean()
    .vertices(cq.selectors.BoxSelector((-W / 2, hz0 - 1, -1.0), (W / 2, hz1 + 1, 1.0)))
    .fillet(CH_R)
)
channel = cq.Workplane("XZ").placeSketch(ch).extrude(CH_DEPTH, taper=CH_TAPER)
body = body.cut(channel)

# V-shaped sloping facet above the upper panels: it starts at the channel
# top (PANEL_TOP) and rises to the top edge towards both sides; its surface
# slopes back out to the top edge so the flange top edge stays straight
y_top = -CH_DEPTH + CH_DEPTH * (H + 1 - PANEL_TOP) / (H - PANEL_TOP)
wedge = (
    cq.Workplane("YZ")
    .polyline([(-CH_DEPTH, PANEL_TOP), (2.0, PANEL_TOP), (2.0, H + 1), (y_top, H + 1)])
    .close()
    .extrude(W, both=True)
)
xc = (vx0 + vx1) / 2
v_slope = (H - PANEL_TOP) / V_REACH
vb = 40.0
vee = (
    cq.Workplane("XZ")
    .polyline([
        (xc - vb, PANEL_TOP + v_slope * vb),
        (xc, PANEL_TOP),
        (xc + vb, PANEL_TOP + v_slope * vb),
        (xc + vb, H + 20),
        (xc - vb, H + 20),
    ])
    .close()
    .extrude(5, both=True)
)
strip = wedge.intersect(vee)
body = body.cut(strip)

try:
    txt_plane = cq.Plane(origin=(TXT_X, 0.0, TXT_Z), xDir=(0, 0, -1), normal=(0, 1, 0))
    txt = cq.Workplane(txt_plane).text(
        TXT, TXT_SIZE, -TXT_DEPTH, combine=False, font="DejaVu Sans",
        halign="center", valign="center",
    )
    for letter in txt.solids().vals():
        body = body.cut(letter)
except Exception:
    pass

result = body
